import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
R_OUT = 50.0          # tyre outer radius
WIDTH = 24.7          # tyre width (along Y, the wheel axis)
TYRE_FILLET = 2.7     # outer corner rounding of the tyre
R_RIM = 33.2          # radius of the recess inside the tyre

# spoke web: flat plate joining hub and rim
WEB_FRONT = -3.0      # y of the front face of the web
WEB_BACK = 3.0        # y of the back face of the web
RECESS_FILLET = 6.0   # blend between rim wall and web

N_SPOKES = 6
WIN_R_IN = 16.5       # inner radius of the windows
WIN_HALF_ANG = 16.0   # half opening angle of each window at the hub (deg)
WIN_HALF_ANG_OUT = 17.7  # half opening angle of each window at the rim (deg)
WIN_ROT = -2.4        # angular offset of the window pattern (deg, from +X to +Z)
WIN_CORNER = 1.2      # window corner radius (in the XZ outline)
WIN_EDGE_FILLET = 0.8 # softening of window edges on the web faces
WIN_OVERCUT = 0.3     # windows reach slightly into the rim wall

R_SHAFT = 8.25        # back shaft / front cap radius
SHAFT_LEN = 20.3      # shaft protrusion beyond back tyre face
SHAFT_CHAMFER = 0.8
SOCKET_L = 11.5       # obround socket overall length
SOCKET_W = 5.6        # obround socket width
SOCKET_DEPTH = 6.0
KEY_L = 12.0          # obround key on the front hub
KEY_W = 6.0
KEY_H = 0.8           # key height above the hub face
SLOT_ANGLE = 40.0     # obround orientation in XZ plane (deg from +X)
CAP_T = 0.3           # front cap (hub disc) thickness, separate body
CAP_PROUD = 0.7       # cap protrusion beyond front tyre face

SEAM_ROT = 135.0      # rotate revolve seams to the hidden lower-back quadrant

HW = WIDTH / 2.0


def xz(y):
    """XZ workplane at axial position y (normal points to -Y)."""
    return cq.Workplane("XZ", origin=(0, y, 0))


class CircleSel(cq.Selector):
    """circular edges of radius r centred on the axis at height y"""

    def __init__(self, r, y, tol=0.05):
        self.r, self.y, self.tol = r, y, tol

    def filter(self, objs):
        out = []
        for e in objs:
            if e.geomType() == "CIRCLE" and abs(e.radius() - self.r) < self.tol \
                    and abs(e.Center().y - self.y) < self.tol:
                out.append(e)
        return out


def web_y(r, front):
    """axial position of the web face"""
    return WEB_FRONT if front else WEB_BACK


# ---------------- wheel body of revolution ----------------
prof = [
    (0.0, WEB_FRONT),
    (R_RIM, WEB_FRONT),
    (R_RIM, -HW),
    (R_OUT, -HW),
    (R_OUT, HW),
    (R_RIM, HW),
    (R_RIM, WEB_BACK),
    (0.0, WEB_BACK),
]
body = (cq.Workplane("XY").polyline(prof).close()
        .revolve(360.0, (0, 0, 0), (0, 1, 0))
        .rotate((0, 0, 0), (0, 1, 0), SEAM_ROT))
body = body.edges(CircleSel(R_OUT, HW)).fillet(TYRE_FILLET)
body = body.edges(CircleSel(R_OUT, -HW)).fillet(TYRE_FILLET)
body = body.edges(CircleSel(R_RIM, WEB_FRONT)).fillet(RECESS_FILLET)
body = body.edges(CircleSel(R_RIM, WEB_BACK)).fillet(RECESS_FILLET)

# ---------------- spoke windows ----------------
# each window is bounded by the hub circle, the rim circle and two straight
# edges that open slightly faster than radial lines (spokes taper outward)
a_in = math.radians(WIN_HALF_ANG)
a_out = math.radians(WIN_HALF_ANG_OUT)
p_in = (WIN_R_IN * math.cos(a_in), WIN_R_IN * math.sin(a_in))
p_out = (R_RIM * math.cos(a_out), R_RIM * math.sin(a_out))
ext = 1.6  # extend the edge line well past the rim circle
p_far = (p_in[0] + ext * (p_out[0] - p_in[0]), p_in[1] + ext * (p_out[1] - p_in[1]))
p_in0 = (p_in[0] - 0.3 * (p_out[0] - p_in[0]), p_in[1] - 0.3 * (p_out[1] - p_in[1]))
win_sketch = (
    cq.Sketch()
    .polygon([
        (0, 0),
        (p_in0[0], p_in0[1]),
        p_far,
        (p_far[0] + 10.0, 0.0),
        (p_far[0], -p_far[1]),
        (p_in0[0], -p_in0[1]),
        (0, 0),
    ])
    .circle(WIN_R_IN, mode="s")
    .circle(R_RIM + WIN_OVERCUT, mode="i")
    .vertices()
    .fillet(WIN_CORNER)
)
windows = None
for i in range(N_SPOKES):
    ang = WIN_ROT + i * 360.0 / N_SPOKES
    w = xz(HW + 1).placeSketch(win_sketch.copy()).extrude(WIDTH + 2)
    w = w.rotate((0, 0, 0), (0, 1, 0), -ang)
    windows = w if windows is None else windows.union(w)
body = body.cut(windows)


class WindowEdgeSel(cq.Selector):
    """non-circular edges lying on a web face (the window mouths)"""

    def __init__(self, front, tol=0.05):
        self.front, self.tol = front, tol

    def filter(self, objs):
        out = []
        for e in objs:
            if e.geomType() == "CIRCLE":
                c = e.Center()
                if math.hypot(c.x, c.z) < 0.01:
                    continue
            ok = True
            for t in (0.0, 0.5, 1.0):
                p = e.positionAt(t)
                r = math.hypot(p.x, p.z)
                if r < WIN_R_IN - 0.5 or r > R_RIM - 0.2:
                    ok = False
                    break
                if abs(p.y - web_y(r, self.front)) > self.tol:
                    ok = False
                    break
            if ok:
                out.append(e)
        return out


body = body.edges(WindowEdgeSel(True)).fillet(WIN_EDGE_FILLET)
body = body.edges(WindowEdgeSel(False)).fillet(WIN_EDGE_FILLET)

# ---------------- back shaft with obround socket ----------------
shaft = (xz(WEB_BACK - 0.5).circle(R_SHAFT).extrude(-(HW - WEB_BACK + 0.5 + SHAFT_LEN))
         .rotate((0, 0, 0), (0, 1, 0), SEAM_ROT))
shaft = shaft.faces(">Y").edges().chamfer(SHAFT_CHAMFER)
body = body.union(shaft)
socket = xz(HW + SHAFT_LEN).slot2D(SOCKET_L, SOCKET_W, SLOT_ANGLE).extrude(SOCKET_DEPTH)
body = body.cut(socket)

# ---------------- front: short obround key + separate thin round cap ----------------
key = xz(WEB_FRONT + 0.5).slot2D(KEY_L, KEY_W, SLOT_ANGLE).extrude(KEY_H + 0.5)
body = body.union(key)
cap = (xz(-HW - CAP_PROUD + CAP_T).circle(R_SHAFT).extrude(CAP_T)
       .rotate((0, 0, 0), (0, 1, 0), SEAM_ROT))

result = cq.Workplane("XY").newObject([cq.Compound.makeCompound([body.val(), cap.val()])])
VIEW = {"azimuth": 45, "elevation": 26}
